import math
import cadquery as cq
from OCP.GC import GC_MakeSegment, GC_MakeArcOfCircle
from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.gp import gp_Pnt
from OCP.BRep import BRep_Tool
from OCP.Geom import Geom_SurfaceOfLinearExtrusion, Geom_BSplineCurve
from OCP.Convert import Convert_ParameterisationType

POLY = Convert_ParameterisationType.Convert_Polynomial

# ---------------- driving dimensions (mm) ----------------
W = 175.0          # overall width (X)
H = 101.3          # front height to the (virtual) sharp top corner (Z)
D = 101.5          # overall depth (Y); front face at y=0, back face at y=D
ALPHA = 29.7       # slope of the top panel (deg), falling toward the back
R_BEND = 17.5      # outer radius of the top/back bend
R_BEND_IN = 13.8   # inner radius of the bend
R_NOSE = 1.3       # rounding of the top panel front edge
T_TOP = 3.7        # top panel thickness
T_BACK = 4.2       # back panel thickness
T_SIDE = 4.4       # side wall thickness
T_FRONT = 4.0      # front wall thickness
T_BOT = 3.0        # bottom plate thickness
CH_BACK = 0.7      # small chamfer on the lower outer edge of the back panel

# ears / mounting tabs on the side walls (in the front plane)
TAB_R = 11.0
TAB_Z = 50.3       # height of the ear centres
TAB_T = 4.2
TAB_HOLE_D = 6.0
TAB_HOLE_OFF = 5.5

# top panel holes (2 rows x 3), perpendicular to the sloped panel
TOP_HOLE_D = 10.0
TOP_HOLE_X = 50.5
TOP_HOLE_Y = (25.1, 62.4)   # horizontal distance from the front face

# back panel features: (x, z, diameter)
BACK_HOLES = [(48.0, 17.3, 6.5), (28.5, 17.3, 9.0), (9.6, 17.3, 6.5), (-59.3, 11.1, 6.5)]
SWITCH = (-59.5, 23.4, 14.0, 5.5)  # x, z, width, height

# engraved labels: (text, x, horizontal distance from front / height, font size)
TEXT_DEPTH = 0.4
TOP_LABELS = [
    ("ECEBORG", 0.0, 8.3, 13.9),
    ("Elbow", -50.5, 38.0, 9.5),
    ("Shoulder", 0.0, 38.0, 9.5),
    ("Waist", 50.5, 38.0, 9.5),
    ("Grip", -50.5, 75.4, 9.5),
    ("Wrist", 0.0, 81.0, 7.0),
    ("Pitch", 0.0, 75.2, 7.0),
    ("Wrist", 50.5, 81.0, 7.0),
    ("Roll", 50.5, 75.2, 7.0),
]
BACK_LABELS = [
    ("Bluetooth", 48.5, 10.7, 5.0),
    ("Load", 7.5, 9.1, 5.0),
    ("ON", -43.6, 23.2, 5.0),
    ("OFF", -75.6, 23.2, 5.0),
]

# bottom plate features
BOT_HOLE_D = 15.0
BOT_HOLE_Y = 18.0
BOT_SMALL_D = 4.2
BOT_SMALL_X = 75.5
BOT_TINY = (-81.0, 8.0, 2.4)   # x, y, diameter of the tiny corner hole

KNOT_STEP = 3.0    # knot spacing of the smooth panel profile (tessellation aid)
KNOT_Y_NOSE = 3.9

VIEW = {"azimuth": 45, "elevation": 26}

ta = math.tan(math.radians(ALPHA))
ca = math.cos(math.radians(ALPHA))
sa = math.sin(math.radians(ALPHA))


# ---------------- 2D profile helpers (profile lives in the YZ plane) ----------------
def _p(x, q):
    return gp_Pnt(x, q[0], q[1])


def _geom(seg, x):
    if len(seg) == 2:
        return GC_MakeSegment(_p(x, seg[0]), _p(x, seg[1])).Value()
    return GC_MakeArcOfCircle(_p(x, seg[0]), _p(x, seg[1]), _p(x, seg[2])).Value()


def smooth_edge(segs, x):
    """Join tangent-continuous lines/arcs into one exact B-spline edge."""
    comp = GeomConvert_CompCurveToBSplineCurve(GeomConvert.CurveToBSplineCurve_s(_geom(segs[0], x), POLY))
    for s in segs[1:]:
        comp.Add(GeomConvert.CurveToBSplineCurve_s(_geom(s, x), POLY), 1e-6)
    return cq.Edge(BRepBuilderAPI_MakeEdge(comp.BSplineCurve()).Edge())


def densify_knots(shape, step=KNOT_STEP):
    """Insert extra knots into the B-spline profile of the smooth panel faces.
    Knot insertion leaves the geometry and its parametrisation untouched; it only
    gives the tessellator a finer grid on the large smooth face.  Done after all
    booleans so that they run on the simplest representation."""
    for f in shape.Faces():
        srf = BRep_Tool.Surface_s(f.wrapped)
        if not isinstance(srf, Geom_SurfaceOfLinearExtrusion) or f.Area() < 5000.0:
            continue  # only the two large panel faces, not the lettering
        bs = srf.BasisCurve()
        if not isinstance(bs, Geom_BSplineCurve) or bs.NbKnots() > 20:
            continue  # not a panel profile, or already refined
        u0, u1 = bs.FirstParameter(), bs.LastParameter()
        n = int((u1 - u0) / (step / 6.0))
        last = None
        for i in range(1, n):
            u = u0 + (u1 - u0) * i / n
            p = bs.Value(u)
            gap = step / 6.0 if (p.Y() < KNOT_Y_NOSE and p.Z() > H / 2) else step
            if last is None or u - last >= gap * 0.999:
                bs.InsertKnot(u, 1, 1e-9)
                last = u
    return shape


def plain_edge(seg, x):
    return cq.Edge(BRepBuilderAPI_MakeEdge(_geom(seg, x)).Edge())


def prism(edges, x0, length):
    wire = cq.Wire.assembleEdges(edges)
    face = cq.Face.makeFromWires(wire)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(length, 0, 0)))


def fillet_corner(line_pt, corner, down_pt, radius):
    """Tangent points and arc midpoint for rounding `corner` between the
    segment toward line_pt and the segment toward down_pt."""
    u1 = (line_pt[0] - corner[0], line_pt[1] - corner[1])
    n1 = math.hypot(*u1)
    u1 = (u1[0] / n1, u1[1] / n1)
    u2 = (down_pt[0] - corner[0], down_pt[1] - corner[1])
    n2 = math.hypot(*u2)
    u2 = (u2[0] / n2, u2[1] / n2)
    theta = math.acos(u1[0] * u2[0] + u1[1] * u2[1])
    L = radius / math.tan(theta / 2)
    t1 = (corner[0] + L * u1[0], corner[1] + L * u1[1])
    t2 = (corner[0] + L * u2[0], corner[1] + L * u2[1])
    bis = (u1[0] + u2[0], u1[1] + u2[1])
    nb = math.hypot(*bis)
    bis = (bis[0] / nb, bis[1] / nb)
    dc = radius / math.sin(theta / 2)
    c = (corner[0] + dc * bis[0], corner[1] + dc * bis[1])
    m = (c[0] - radius * bis[0], c[1] - radius * bis[1])
    return t1, m, t2


# ---------------- key profile points ----------------
z_in_front = H - T_TOP / ca                       # inner slope height at y=0 (seam)
# outer sharp corners
q_back = (D, H - D * ta)
# inner sharp corner
yb_in = D - T_BACK
q_back_in = (yb_in, z_in_front - yb_in * ta)

# outer front nose (vertical front -> slope)
zc = H - R_NOSE * (1 + sa) / ca
nose_a = (0.0, zc)
nose_b = (R_NOSE * (1 + sa), zc + R_NOSE * ca)
nb_dir = (-1 + sa, ca)
nbn = math.hypot(*nb_dir)
nose_m = (R_NOSE + R_NOSE * nb_dir[0] / nbn, zc + R_NOSE * nb_dir[1] / nbn)

# outer bend
b1, bm, b2 = fillet_corner((0.0, H), q_back, (D, 0.0), R_BEND)
# inner bend
i1, im, i2 = fillet_corner((0.0, z_in_front), q_back_in, (yb_in, 0.0), R_BEND_IN)

X0 = -W / 2


def top_back_panel():
    outer = smooth_edge([
        [(0.0, z_in_front), nose_a],
        [nose_a, nose_m, nose_b],
        [nose_b, b1],
        [b1, bm, b2],
        [b2, (D, CH_BACK)],
    ], X0)
    edges = [
        outer,
        plain_edge([(D, CH_BACK), (D - CH_BACK, 0.0)], X0),
        plain_edge([(D - CH_BACK, 0.0), (yb_in, 0.0)], X0),
        smooth_edge([
            [(yb_in, 0.0), i2],
            [i2, im, i1],
            [i1, (0.0, z_in_front)],
        ], X0),
    ]
    return prism(edges, X0, W)


def inner_region(x0, length):
    edges = [
        plain_edge([(0.0, 0.0), (0.0, z_in_front)], x0),
        smooth_edge([
            [(0.0, z_in_front), i1],
            [i1, im, i2],
            [i2, (yb_in, 0.0)],
        ], x0),
        plain_edge([(yb_in, 0.0), (0.0, 0.0)], x0),
    ]
    return prism(edges, x0, length)


# ---------------- top / back bent panel ----------------
panel = top_back_panel()

nrm = cq.Vector(0, sa, ca)
for yh in TOP_HOLE_Y:
    zh = H - yh * ta
    for xh in (-TOP_HOLE_X, 0.0, TOP_HOLE_X):
        p = cq.Vector(xh, yh, zh) - nrm * 10
        panel = panel.cut(cq.Workplane().add(cq.Solid.makeCylinder(TOP_HOLE_D / 2, 20, p, nrm)))

for xh, zh, dh in BACK_HOLES:
    cyl = cq.Solid.makeCylinder(dh / 2, 20, cq.Vector(xh, D - 10, zh), cq.Vector(0, 1, 0))
    panel = panel.cut(cq.Workplane().add(cyl))
sx, sz, sw, sh = SWITCH
panel = panel.cut(cq.Workplane("XY").box(sw, 20, sh).translate((sx, D, sz)))


# ---------------- engraved labels ----------------
def _label_solid(origin, xdir, out_normal, txt, size, mirrored=False):
    """Letters cut TEXT_DEPTH deep into a surface with outward normal `out_normal`.
    They start 0.5 mm outside the surface to avoid coincident faces."""
    n = cq.Vector(out_normal)
    o = cq.Vector(origin) + n * 0.5
    if mirrored:  # sketched from the inside: reads mirrored from outside
        pl = cq.Plane(origin=o, xDir=xdir, normal=-n)
        dist = TEXT_DEPTH + 0.5
    else:
        pl = cq.Plane(origin=o, xDir=xdir, normal=n)
        dist = -(TEXT_DEPTH + 0.5)
    return cq.Workplane(pl).text(txt, size, dist, combine=False, clean=True,
                                 halign="center", valign="center").val()


def engrave_labels(body):
    solids = []
    for txt, x, y, size in TOP_LABELS:
        z = H - y * ta
        solids.append(_label_solid((x, y, z), (1, 0, 0), (0, sa, ca), txt, size))
    for txt, x, z, size in BACK_LABELS:
        # the back labels of the original read mirrored from behind
        solids.append(_label_solid((x, D, z), (1, 0, 0), (0, 1, 0), txt, size, mirrored=True))
    return body.cut(cq.Workplane().add(cq.Compound.makeCompound(solids)))


try:
    panel = engrave_labels(panel)
except Exception:  # fonts unavailable -> keep the plain panel
    pass
panel = cq.Workplane("XY").add(densify_knots(panel.val()))


# ---------------- side walls with ears ----------------
def side_wall(sign):
    x_out = sign * W / 2
    x0 = W / 2 - T_SIDE if sign > 0 else -W / 2
    wall = inner_region(x0, T_SIDE)
    ear = (
        cq.Workplane("XZ")
        .center(x_out, TAB_Z)
        .circle(TAB_R)
        .extrude(-TAB_T)
    )
    keep = cq.Workplane("XY").box(TAB_R * 2, TAB_T * 3, TAB_R * 3).translate(
        (x_out + sign * TAB_R, 0, TAB_Z))
    ear = ear.intersect(keep)
    hole = (
        cq.Workplane("XZ")
        .center(x_out + sign * TAB_HOLE_OFF, TAB_Z)
        .circle(TAB_HOLE_D / 2)
        .extrude(TAB_T * 3, both=True)
    )
    ear = ear.cut(hole)
    if sign > 0:
        return [wall.union(ear)]
    # the left ear is a separate body (its front face shows a seam line)
    return [wall, ear]


left = side_wall(-1)
right = side_wall(1)

# ---------------- front wall (between the side walls, under the top panel) ----------------
xf = -W / 2 + T_SIDE
front = prism([
    plain_edge([(0.0, 0.0), (0.0, z_in_front)], xf),
    plain_edge([(0.0, z_in_front), (T_FRONT, z_in_front - T_FRONT * ta)], xf),
    plain_edge([(T_FRONT, z_in_front - T_FRONT * ta), (T_FRONT, 0.0)], xf),
    plain_edge([(T_FRONT, 0.0), (0.0, 0.0)], xf),
], xf, W - 2 * T_SIDE)

# ---------------- bottom plate ----------------
bottom = (
    cq.Workplane("XY")
    .box(W - 2 * T_SIDE, yb_in - T_FRONT, T_BOT, centered=(True, False, False))
    .translate((0, T_FRONT, 0))
)
bottom = bottom.cut(
    cq.Workplane("XY").center(0, BOT_HOLE_Y).circle(BOT_HOLE_D / 2).extrude(T_BOT * 3, both=True)
)
bottom = bottom.cut(
    cq.Workplane("XY").pushPoints([(-BOT_SMALL_X, D / 2), (BOT_SMALL_X, D / 2)])
    .circle(BOT_SMALL_D / 2).extrude(T_BOT * 3, both=True)
)
bottom = bottom.cut(
    cq.Workplane("XY").center(BOT_TINY[0], BOT_TINY[1])
    .circle(BOT_TINY[2] / 2).extrude(T_BOT * 3, both=True)
)

parts = [panel] + left + right + [front, bottom]
solids = [so for p in parts for so in p.val().Solids()]
result = cq.Workplane("XY").add(cq.Compound.makeCompound(solids))
